import math
import cadquery as cq

# ---------------------------------------------------------------- parameters
# lower hub ring (vertical axis = Z, hub axis at X=Y=0, Z=0 at the bottom)
R_RING_LO = 39.8      # lower band radius
H_RING_LO = 15.2      # lower band height
R_GROOVE = 38.0       # groove root radius
H_GROOVE = 0.7
R_RING_UP = 38.8      # upper band radius
FLAT_Y = 37.0         # wrench flats on the upper band
FLAT_Z0 = 17.0
RADIAL_HOLE_Z = 9.7
RADIAL_HOLE_D = 3.4
RADIAL_CB_D = 7.0
BOT_HOLE_R = 19.0     # six holes on the bottom face
BOT_HOLE_D = 3.8
BOT_GROOVE_R = 30.5   # C shaped groove on the bottom face
BOT_GROOVE_W = 1.4
BOT_GAP_ANG = 29.0
NOTCH_W, NOTCH_H, NOTCH_DEPTH = 3.0, 6.0, 4.0

# clamp housing + arm tube
Z_HB = 24.5           # housing bottom
Z_HT = 65.0           # housing top
R_HOUSING = 44.0
HOUSING_FILLET = 1.5
EAR_X = -56.0         # clamp ear end
EAR_HALF_W = 8.5
EAR_R = 11.0          # rounding of the ear end (XZ)
SLIT_W = 1.4
EAR_HOLE_X = -50.0
EAR_HOLE_D = 3.4
R_TUBE = (Z_HT - Z_HB) / 2.0
Z_TUBE = (Z_HT + Z_HB) / 2.0
R_BORE = 15.3
X_TUBE_END = 180.7
BORE_DEPTH = 110.0
FLARE_RF = 50.0       # plan radius of the concave blend housing -> tube
# loft sections (x, top corner radius, bottom corner radius, inset of the half width)
FLARE_SECTIONS = [(18.0, 0.5, 1.5, 0.5), (27.0, 1.0, 2.0, 0.1), (37.0, 4.5, 5.5, 0.0),
                  (49.0, 11.5, 12.0, 0.0)]

# neck between housing and plate
R_NECK = 39.3
WEB_HALF_W = 15.0
Z_PB = 70.5           # plate bottom
T_PLATE = 11.0
Z_PT = Z_PB + T_PLATE # plate top

# diamond plate
PLATE_HALF_L = 101.8  # half length along Y (to end faces)
END_HALF_W = 14.2     # half width of the plate ends / end blocks
DIAMOND_Y_END = 84.0  # where the straight end part starts widening
DIAMOND_HALF_W = 42.0 # half width at Y = 0
LENS_C = 21.9         # the hub part of the outline: two R65 arcs
LENS_R = 65.0
CB_HOLE_R = 34.7      # four countersunk holes
CB_HOLE_ANG = 30.0
CB_HOLE_D = 3.8
CB_CB_D = 8.6
TAB_X = -55.8
TAB_HALF_W = 13.8
TAB_HOLE_Y = 8.2
TAB_HOLE_X = -50.2
TAB_HOLE_D = 3.0
TAB_STEP = 1.5
TAB_ROOT_X = -41.5
OUTLINE_FILLET = 10.0
TAB_FILLET = 3.0
PLATE_EDGE_FILLET = 2.5

# centre disc recess + holes
DISC_R = 27.2
DISC_DEPTH = 1.0
DISC_R2 = 25.3
DISC_STEP = 0.8
DISC_SMALL_R = 19.0
DISC_SMALL_D = 2.4
DISC_MID_R = 17.0
DISC_MID_D = 4.6
UNDER_RAIL_Y, UNDER_RAIL_W, UNDER_RAIL_H = 16.5, 12.5, 8.5
KIDNEY_OFF, KIDNEY_D1, KIDNEY_D2 = 3.6, 11.0, 9.6

# lugs, spines, rail, end blocks
LUG_Y0, LUG_Y1 = 25.0, 43.0
LUG_W0, LUG_W1 = 10.5, 17.5
LUG_H = 6.0
SPINE_Y0 = 38.0
ROOF_END_R = 44.0
END_Y0 = 87.0
SPINE_HALF_W = 13.0
END_FILLET_R = 7.0
SPINE_TOP = 89.5
RAIL_HALF_W = 5.0
RAIL_NECK_HALF_W = 3.6
RAIL_DOVE_Z0 = 92.6
RAIL_DOVE_Z1 = 95.8
RAIL_TOP = 96.5
END_TOP = 97.5
CHANNEL_FLOOR = 91.0
END_EDGE_R = 3.0
RAIL_HOLE_PITCH = 20.7
RAIL_HOLE_D = 3.0
RAIL_CB_D = 5.6

# underside pockets in the plate arms
POCKET_DEPTH = 6.0
RIB = 1.5
WALL = 1.8
POCKET_Y = [(42.0, 63.0), (66.0, 86.3)]
POCKET_FILLET = 2.0


def diamond_half_width(y):
    y = abs(y)
    if y >= DIAMOND_Y_END:
        return END_HALF_W
    return END_HALF_W + (DIAMOND_HALF_W - END_HALF_W) * (DIAMOND_Y_END - y) / DIAMOND_Y_END


# ---------------------------------------------------------------- lower hub ring
ring = cq.Workplane("XY").circle(R_RING_LO).extrude(H_RING_LO)
ring = ring.union(
    cq.Workplane("XY").workplane(offset=H_RING_LO).circle(R_GROOVE).extrude(H_GROOVE))
ring = ring.union(
    cq.Workplane("XY").workplane(offset=H_RING_LO + H_GROOVE).circle(R_RING_UP)
    .extrude(Z_HB - H_RING_LO - H_GROOVE + 1.0))
ring = ring.faces("<Z").edges().chamfer(0.8)
ring = ring.rotate((0, 0, 0), (0, 0, 1), 180)
# small key notch at the bottom of the ring on the -X side
notch = (cq.Workplane("YZ", origin=(-R_RING_LO - 1, 0, -1)).center(0, NOTCH_H / 2)
         .slot2D(NOTCH_H * 2, NOTCH_W, angle=90).extrude(NOTCH_DEPTH + 1))
ring = ring.cut(notch)

# wrench flats on the upper band
for s in (1, -1):
    ring = ring.cut(
        cq.Workplane("XY").box(40, 10, Z_HB - FLAT_Z0 + 1.0, centered=(True, False, False))
        .translate((0, 0, FLAT_Z0)).translate((0, FLAT_Y if s > 0 else -FLAT_Y - 10, 0)))

# radial counterbored holes on the 45 degree diagonals
for k in range(4):
    a = math.radians(45 + 90 * k)
    d = cq.Vector(math.cos(a), math.sin(a), 0)
    p = cq.Vector(d.x * (R_RING_LO + 1), d.y * (R_RING_LO + 1), RADIAL_HOLE_Z)
    h = cq.Solid.makeCylinder(RADIAL_HOLE_D / 2, 12, p, -d)
    cb = cq.Solid.makeCylinder(RADIAL_CB_D / 2, 2.2, p, -d)
    ring = ring.cut(cq.Workplane().add(h)).cut(cq.Workplane().add(cb))

# six holes + C groove on the bottom face
ring = ring.cut(
    cq.Workplane("XY").polarArray(BOT_HOLE_R, 45, 360, 6).circle(BOT_HOLE_D / 2).extrude(6))
groove = (cq.Workplane("XY").circle(BOT_GROOVE_R + BOT_GROOVE_W / 2)
          .circle(BOT_GROOVE_R - BOT_GROOVE_W / 2).extrude(1.5))
gap = (cq.Workplane("XY").box(20, 60, 4, centered=(False, True, False))
       .translate((BOT_GROOVE_R - 12, 0, -1)).rotate((0, 0, 0), (0, 0, 1), BOT_GAP_ANG))
ring = ring.cut(groove.cut(gap))

# ---------------------------------------------------------------- housing + flare + ear
# plan outline: housing circle blended into the tube width by two concave arcs
_D = R_HOUSING + FLARE_RF
_XC = math.sqrt(_D ** 2 - (R_TUBE + FLARE_RF) ** 2)          # arc meets the tube line here
_TX, _TY = _XC * R_HOUSING / _D, (R_TUBE + FLARE_RF) * R_HOUSING / _D   # meets the circle here

housing = (cq.Workplane("XY").workplane(offset=Z_HB).circle(R_HOUSING).extrude(Z_HT - Z_HB)
           .faces("<Z").edges().fillet(HOUSING_FILLET))


# loft sections: rounded rectangles turning into the tube circle
def _rr_wire(x, a, b, rt, rb):
    """rounded rectangle in the plane X = x (local u = Y, v = Z about the tube axis),
    top corner radius rt, bottom corner radius rb"""
    c = math.cos(math.pi / 4)
    P = lambda u, v: cq.Vector(x, u, Z_TUBE + v)
    e = [
        cq.Edge.makeLine(P(a, -(b - rb)), P(a, b - rt)),
        cq.Edge.makeThreePointArc(P(a, b - rt), P(a - rt + rt * c, b - rt + rt * c), P(a - rt, b)),
        cq.Edge.makeLine(P(a - rt, b), P(-(a - rt), b)),
        cq.Edge.makeThreePointArc(P(-(a - rt), b), P(-(a - rt) - rt * c, b - rt + rt * c), P(-a, b - rt)),
        cq.Edge.makeLine(P(-a, b - rt), P(-a, -(b - rb))),
        cq.Edge.makeThreePointArc(P(-a, -(b - rb)), P(-(a - rb) - rb * c, -(b - rb) - rb * c), P(-(a - rb), -b)),
        cq.Edge.makeLine(P(-(a - rb), -b), P(a - rb, -b)),
        cq.Edge.makeThreePointArc(P(a - rb, -b), P(a - rb + rb * c, -(b - rb) - rb * c), P(a, -(b - rb))),
    ]
    return cq.Wire.assembleEdges(e)


def _circ8_wire(x, R, a, b, rt, rb):
    """circle split into 8 arcs whose vertices match the rounded rectangle ones"""
    P = lambda t: cq.Vector(x, R * math.cos(t), Z_TUBE + R * math.sin(t))
    t1 = math.atan2(b - rt, a)
    t2 = math.atan2(b, a - rt)
    t3 = math.atan2(b - rb, a)
    t4 = math.atan2(b, a - rb)
    ts = [-t3, t1, t2, math.pi - t2, math.pi - t1, math.pi + t3, math.pi + t4,
          2 * math.pi - t4, 2 * math.pi - t3]
    e = []
    for i in range(8):
        t0, t9 = ts[i], ts[i + 1]
        e.append(cq.Edge.makeThreePointArc(P(t0), P((t0 + t9) / 2), P(t9)))
    return cq.Wire.assembleEdges(e)


def _flare_half_width(x):
    if x <= _TX:
        return math.sqrt(R_HOUSING ** 2 - x ** 2)
    if x >= _XC:
        return R_TUBE
    return R_TUBE + FLARE_RF - math.sqrt(FLARE_RF ** 2 - (x - _XC) ** 2)


# smooth loft from a rounded rectangle inside the housing to the tube circle;
# section widths follow the concave plan arcs, corner radii grow into the circle
_bz = R_TUBE - 0.05
_wires = []
for (fx, frt, frb, inset) in FLARE_SECTIONS:
    _wires.append(_rr_wire(fx, _flare_half_width(fx) - inset, _bz, frt, frb))
_lx, _lrt, _lrb, _li = FLARE_SECTIONS[-1]
for fx in (_XC,):
    _wires.append(_circ8_wire(fx, R_TUBE, _flare_half_width(_lx) - _li, _bz, _lrt, _lrb))
flare = cq.Workplane().add(cq.Solid.makeLoft(_wires, False))
housing = housing.union(flare)

ear = (cq.Workplane("XY").box(-EAR_X - 28.0, 2 * EAR_HALF_W, Z_HT - Z_HB,
                              centered=(False, True, False))
       .translate((EAR_X, 0, Z_HB)))
ear = ear.edges("|Y and <X").fillet(EAR_R)
housing = housing.union(ear)

tube = (cq.Workplane("YZ", origin=(_XC - 0.5, 0, Z_TUBE)).circle(R_TUBE)
        .extrude(X_TUBE_END - _XC + 0.5))
tube = tube.faces(">X").edges().fillet(1.5)
arm = housing.union(tube)

# tube bore with a small entry chamfer
arm = arm.cut(cq.Workplane("YZ", origin=(X_TUBE_END, 0, Z_TUBE)).circle(R_BORE)
              .extrude(-BORE_DEPTH))
arm = arm.cut(cq.Workplane().add(cq.Solid.makeCone(
    R_BORE + 1.5, R_BORE - 0.01, 1.51, cq.Vector(X_TUBE_END + 0.5, 0, Z_TUBE), cq.Vector(-1, 0, 0))))

# clamp slit and cross hole through the ear
arm = arm.cut(cq.Workplane("XY").box(-EAR_X - 40.0 + 2, SLIT_W, Z_HT - Z_HB + 4,
                                      centered=(False, True, False))
              .translate((EAR_X - 1, 0, Z_HB - 2)))
arm = arm.cut(cq.Workplane("XZ", origin=(EAR_HOLE_X, EAR_HALF_W + 2, Z_TUBE))
              .circle(EAR_HOLE_D / 2).extrude(2 * EAR_HALF_W + 4))
for s in (1, -1):
    arm = arm.cut(cq.Workplane("XZ", origin=(EAR_HOLE_X, s * (EAR_HALF_W + 1), Z_TUBE))
                  .circle(2.9).extrude(2.5 if s > 0 else -2.5))

# ---------------------------------------------------------------- neck
neck = (cq.Workplane("XY").workplane(offset=Z_HT - 2).circle(R_NECK)
        .extrude(Z_PB - Z_HT + 2.5))
web = (cq.Workplane("XY").box(2 * WEB_HALF_W, 2 * R_HOUSING, Z_PB - Z_HT + 2.5,
                              centered=(True, True, False)).translate((0, 0, Z_HT - 2)))
web = web.intersect(cq.Workplane("XY").workplane(offset=Z_HT - 3).circle(R_HOUSING).extrude(10))
neck = neck.union(web)

# ---------------------------------------------------------------- diamond plate
dia_pts = [
    (END_HALF_W, PLATE_HALF_L), (END_HALF_W, DIAMOND_Y_END), (DIAMOND_HALF_W, 0),
    (END_HALF_W, -DIAMOND_Y_END), (END_HALF_W, -PLATE_HALF_L),
    (-END_HALF_W, -PLATE_HALF_L), (-END_HALF_W, -DIAMOND_Y_END), (-DIAMOND_HALF_W, 0),
    (-END_HALF_W, DIAMOND_Y_END), (-END_HALF_W, PLATE_HALF_L)]
boss_pts = []
for a in (CB_HOLE_ANG, 180 - CB_HOLE_ANG, 180 + CB_HOLE_ANG, -CB_HOLE_ANG):
    r = math.radians(a)
    boss_pts.append((CB_HOLE_R * math.cos(r), CB_HOLE_R * math.sin(r)))

# outline = diamond arms  +  lens of two large arcs around the hub  +  tab
lens = (cq.Workplane("XY").workplane(offset=Z_PB).center(-LENS_C, 0).circle(LENS_R).extrude(T_PLATE)
        .intersect(cq.Workplane("XY").workplane(offset=Z_PB).center(LENS_C, 0).circle(LENS_R)
                   .extrude(T_PLATE)))
plate = (cq.Workplane("XY").workplane(offset=Z_PB).polyline(dia_pts).close().extrude(T_PLATE)
         .union(lens)
         .union(cq.Workplane("XY").workplane(offset=Z_PB).center((TAB_X - 30.0) / 2, 0)
                .rect(-TAB_X - 30.0, 2 * TAB_HALF_W).extrude(T_PLATE)))
_tab_box = cq.selectors.BoxSelector((-80, -40, Z_PB - 5), (-40, 40, Z_PT + 5))
plate = plate.edges("|Z").edges(_tab_box).fillet(TAB_FILLET)
plate = plate.edges("|Z").edges(cq.selectors.InverseSelector(_tab_box)).fillet(OUTLINE_FILLET)
plate = plate.faces(">Z").edges().fillet(PLATE_EDGE_FILLET)
# the tab is a little thinner than the plate
_tab_cut = (cq.Workplane("XY").box(25, 2 * TAB_HALF_W, 5, centered=(False, True, False))
            .translate((TAB_ROOT_X - 25, 0, Z_PT - TAB_STEP))
            .cut(cq.Workplane("XY").workplane(offset=Z_PT - TAB_STEP - 1).circle(-TAB_ROOT_X).extrude(8)))
plate = plate.cut(_tab_cut)

# underside pockets in the arms
for sy in (1, -1):
    for sx in (1, -1):
        for (y0, y1) in POCKET_Y:
            x0 = diamond_half_width(y0) - WALL * 1.05
            x1 = diamond_half_width(y1) - WALL * 1.05
            pts = [(sx * RIB, sy * y0), (sx * x0, sy * y0), (sx * x1, sy * y1), (sx * RIB, sy * y1)]
            pk = (cq.Workplane("XY").workplane(offset=Z_PB - 1).polyline(pts).close()
                  .extrude(POCKET_DEPTH + 1).edges("|Z").fillet(1.5)
                  .faces(">Z").edges().fillet(POCKET_FILLET))
            plate = plate.cut(pk)

# ---------------------------------------------------------------- lugs, spines, end blocks
lugs = None
for sy in (1, -1):
    pts = [(-LUG_W0, sy * LUG_Y0), (LUG_W0, sy * LUG_Y0), (LUG_W1, sy * LUG_Y1), (-LUG_W1, sy * LUG_Y1)]
    lug = (cq.Workplane("XY").workplane(offset=Z_PT - 0.5).polyline(pts).close()
           .extrude(LUG_H + 0.5).edges("|Z").fillet(2.5).faces(">Z").edges().fillet(1.0))
    lugs = lug if lugs is None else lugs.union(lug)

# ridge under the rail on each arm: concave coves down to the plate
spines = None
for sy in (1, -1):
    y0, y1 = SPINE_Y0, END_Y0 + 1
    sp = (cq.Workplane("XY").box(2 * SPINE_HALF_W, y1 - y0, SPINE_TOP - Z_PT + 0.5,
                                 centered=(True, False, False))
          .translate((0, y0, Z_PT - 0.5)))
    for sx in (1, -1):
        cyl = (cq.Workplane("XZ", origin=(sx * SPINE_HALF_W, y1 + 1, SPINE_TOP))
               .circle(SPINE_HALF_W - RAIL_HALF_W).extrude(y1 - y0 + 2))
        sp = sp.cut(cyl)
    if sy < 0:
        sp = sp.mirror("XZ")
    spines = sp if spines is None else spines.union(sp)
# the ridges end on a cylinder around the hub, just outside the lugs
spines = spines.cut(cq.Workplane("XY").workplane(offset=Z_PT - 1).circle(ROOF_END_R).extrude(12))

ends = None
for sy in (1, -1):
    eb = (cq.Workplane("XY").box(2 * END_HALF_W, PLATE_HALF_L - END_Y0, END_TOP - Z_PB,
                                 centered=(True, False, False))
          .translate((0, END_Y0, Z_PB)))
    eb = eb.edges("|Z").fillet(END_EDGE_R).faces(">Z").edges().fillet(1.0)
    if sy < 0:
        eb = eb.mirror("XZ")
    ends = eb if ends is None else ends.union(eb)

# concave fillet where the arms run into the end blocks
for sy in (1, -1):
    fb = (cq.Workplane("XY").box(2 * END_HALF_W, END_FILLET_R, END_FILLET_R, centered=(True, False, False))
          .translate((0, END_Y0 - END_FILLET_R, Z_PT - 0.01)))
    fb = fb.cut(cq.Workplane("YZ", origin=(-END_HALF_W - 1, END_Y0 - END_FILLET_R, Z_PT + END_FILLET_R))
                .circle(END_FILLET_R).extrude(2 * END_HALF_W + 2))
    if sy < 0:
        fb = fb.mirror("XZ")
    spines = spines.union(fb)

top = plate.union(lugs).union(spines)

# centre disc recess (also trims the inner ends of the lugs)
top = top.cut(cq.Workplane("XY").workplane(offset=Z_PT - DISC_DEPTH).circle(DISC_R)
              .extrude(LUG_H + DISC_DEPTH + 1))
top = top.cut(cq.Workplane("XY").workplane(offset=Z_PT - DISC_DEPTH - DISC_STEP).circle(DISC_R2)
              .extrude(DISC_STEP + 0.1))

top = top.union(ends)
# rail channel through the end blocks (rail top sits just below the cheeks)
top = top.cut(cq.Workplane("XY").box(2 * RAIL_HALF_W, 2 * PLATE_HALF_L + 2, END_TOP - CHANNEL_FLOOR + 2,
                                     centered=(True, True, False)).translate((0, 0, CHANNEL_FLOOR)))

# rail: dovetail section (X, Z), extruded along Y over the full plate length
rail_sec = [(-RAIL_NECK_HALF_W, SPINE_TOP - 0.3), (RAIL_NECK_HALF_W, SPINE_TOP - 0.3),
            (RAIL_NECK_HALF_W, RAIL_DOVE_Z0), (RAIL_HALF_W, RAIL_DOVE_Z1),
            (RAIL_HALF_W - 0.6, RAIL_TOP), (-RAIL_HALF_W + 0.6, RAIL_TOP),
            (-RAIL_HALF_W, RAIL_DOVE_Z1), (-RAIL_NECK_HALF_W, RAIL_DOVE_Z0)]
rail = (cq.Workplane("XZ", origin=(0, PLATE_HALF_L, 0)).polyline(rail_sec).close()
        .extrude(2 * PLATE_HALF_L))
top = top.union(rail)

# ---------------------------------------------------------------- holes in the top
Z_CUT = Z_PT + 0.01
# disc: six small holes, two medium holes, two kidney openings
top = top.cut(cq.Workplane("XY").workplane(offset=Z_CUT - DISC_DEPTH)
              .polarArray(DISC_SMALL_R, 0, 360, 6).circle(DISC_SMALL_D / 2).extrude(-16))
mids = []
kid = []
for a in (210, 330):
    r = math.radians(a)
    mids.append((DISC_MID_R * math.cos(r), DISC_MID_R * math.sin(r)))
for a in (30, 150):
    r = math.radians(a)
    kid.append((DISC_MID_R * math.cos(r), DISC_MID_R * math.sin(r)))
top = top.cut(cq.Workplane("XY").workplane(offset=Z_CUT - DISC_DEPTH).pushPoints(mids)
              .circle(DISC_MID_D / 2).extrude(-16))
for (kx, ky) in kid:
    ang = math.degrees(math.atan2(ky, kx))
    ca, sa = math.cos(math.radians(ang)), math.sin(math.radians(ang))
    ks = (cq.Sketch().push([(-KIDNEY_OFF * ca, -KIDNEY_OFF * sa)]).circle(KIDNEY_D1 / 2)
          .push([(KIDNEY_OFF * ca, KIDNEY_OFF * sa)]).circle(KIDNEY_D2 / 2).reset().clean())
    top = top.cut(cq.Workplane("XY").workplane(offset=Z_CUT - DISC_DEPTH - DISC_STEP - 17)
                  .center(kx, ky).placeSketch(ks).extrude(17.2))

# opening through the disc under the rail next to the -Y lug
top = top.cut(cq.Workplane("XY").workplane(offset=Z_CUT - DISC_DEPTH - DISC_STEP - 17)
              .center(0, -UNDER_RAIL_Y).rect(UNDER_RAIL_W, UNDER_RAIL_H).extrude(17.2)
              .edges("|Z").fillet(3.0))

# four countersunk holes around the disc
top = top.cut(cq.Workplane("XY").workplane(offset=Z_CUT).pushPoints(boss_pts)
              .circle(CB_HOLE_D / 2).extrude(-18))
for (bx, by) in boss_pts:
    r1 = CB_CB_D / 2 + 0.5
    cone = cq.Solid.makeCone(r1, CB_HOLE_D / 2 - 0.2, r1 - CB_HOLE_D / 2 + 0.2,
                             cq.Vector(bx, by, Z_PT + 0.5), cq.Vector(0, 0, -1))
    top = top.cut(cq.Workplane().add(cone))
# tab holes
top = top.cut(cq.Workplane("XY").workplane(offset=Z_CUT)
              .pushPoints([(TAB_HOLE_X, TAB_HOLE_Y), (TAB_HOLE_X, -TAB_HOLE_Y)])
              .circle(TAB_HOLE_D / 2).extrude(-T_PLATE - 1))
# rail holes
rail_pts = [(0, (i + 0.5) * RAIL_HOLE_PITCH * s) for i in range(5) for s in (1, -1)]
top = top.cut(cq.Workplane("XY").workplane(offset=RAIL_TOP + 0.01).pushPoints(rail_pts)
              .circle(RAIL_HOLE_D / 2).extrude(-(RAIL_TOP - SPINE_TOP) - 2))
top = top.cut(cq.Workplane("XY").workplane(offset=RAIL_TOP + 0.01).pushPoints(rail_pts)
              .circle(RAIL_CB_D / 2).extrude(-1.6))

# ---------------------------------------------------------------- assemble
result = ring.union(arm).union(neck).union(top)

VIEW = {"azimuth": 45, "elevation": 26}
